import math
import cadquery as cq

# ---------------------------------------------------------------
# Exploded kit of six parts laid out in the XZ plane, all resting
# against a common "table" plane at Y = Y_TABLE (front faces).
# ---------------------------------------------------------------
Y_TABLE = -4.3

# ---------- 1. ball-end L hex key ----------
HK_AF = 7.9                      # across flats
HK_R = HK_AF / math.sqrt(3.0)    # circumradius
HK_TOP = 116.9                   # top of ball
HK_SHAFT_TOP = 106.2             # end of hex shaft
HK_STEP_Z = 26.5                 # change of section on the long arm
HK_ROT = 15.0                    # rotation of the hex section (deg)
HK_TIP_CH = 1.6                  # chamfer on the short leg tip
HK_LEG_Z = -60.2                 # short leg centre line Z
HK_LEG_END = 31.8                # short leg end X
HK_BEND_R = 7.5                  # bend centre-line radius
HK_BALL_R = 4.5
HK_NECK_R = 2.8

# ---------- 2. rod end ----------
RE_START = (29.9, 90.0)          # hex end centre (X, Z)
RE_ANGLE = 10.5                  # axis tilt (deg, eye end down)
RE_Y = 4.15                      # axis Y
RE_HEX_AF = 17.0
RE_HEX_L = 6.6
RE_SHANK_D = 16.0
RE_SHANK_L = 37.0
RE_EYE_X = 50.6                  # eye centre along axis
RE_EYE_R = 15.0
RE_EYE_T = 11.6
RE_EYE_FILLET = 2.4
RE_FLAT_X = 37.0                 # start of the flats near the eye
RE_BALL_SR = 11.0
RE_BALL_W = 16.2
RE_HOUSING_R = 10.1
RE_BORE_R = 6.0

# ---------- 3. bushing / roller ----------
BU_X0, BU_X1 = 20.2, 59.8
BU_R = 13.4
BU_YC = Y_TABLE + BU_R
BU_ZC = 39.8
BU_BORE_R = 3.8
BU_SEAL_RO, BU_SEAL_RI = 7.3, 5.2

# ---------- 4. angle bracket ----------
AB_W = 46.5                      # leg width along X
AB_H = 46.5                      # height
AB_D = 47.1                      # side leg depth along Y
AB_T = 7.8
AB_CX, AB_CZ = 65.9, -23.7       # centre of front face
AB_ANGLE = -3.8

# ---------- 5. two-bolt flange bearing ----------
FB_CX, FB_CZ = 91.0, -86.0
FB_ANGLE = -62.3
FB_HOLE_D = 17.45                # half bolt spacing
FB_RC = 12.4                     # central radius
FB_RE = 5.6                      # end radius
FB_T = 6.6
FB_Y_FRONT = -4.6
FB_BOSS_H = 0.8
FB_BOLT_D = 4.0
FB_RING_RO, FB_RING_RI = 10.2, 7.6
FB_BORE_R = 5.6
FB_SEAT_RO, FB_SEAT_RI, FB_SEAT_D = 9.0, 6.6, 1.6

# ---------- 6. handle / latch ----------
HD_ORIGIN = (-17.9, Y_TABLE, -107.6)
HD_ANGLE = 8.0
HD_L, HD_T, HD_H = 80.5, 10.0, 24.0
HD_WALL = 4.0                    # front wall behind the back channel
HD_LIP = 1.6                     # thin lip left at full height
HD_STEP = 1.8                    # lowering of the middle top
HD_RIM = 1.8                     # rim over the back channel
HD_END_L, HD_END_R = 14.0, 6.0   # end wall lengths
HD_BASE_Y0, HD_BASE_Y1, HD_BASE_H = 6.0, 27.0, 7.0
HD_RAIL_H = 3.5
HD_RAIL_X0, HD_RAIL_X1, HD_RAIL_Y0 = 16.5, 64.0, 19.0
HD_HOLE_Y, HD_HOLE_Z = 34.0, 1.8
HD_LUGS = (21.0, 49.5)
HD_LUG_W = 8.0
HD_LUG_Y1 = 41.5
HD_LUG_TOP = 6.5
HD_HOLE_D = 3.5


def hexagon_pts(r, start_deg):
    return [(r * math.cos(math.radians(start_deg + 60 * k)),
             r * math.sin(math.radians(start_deg + 60 * k))) for k in range(6)]


# ================= 1. hex key =================
def make_hex_key():
    z_bend = HK_LEG_Z + HK_BEND_R
    pts = hexagon_pts(HK_R, HK_ROT)      # hex section of the arm
    pts_up = hexagon_pts(HK_R * 0.95, HK_ROT)  # slightly thinner upper section
    # long vertical arm, lower section
    arm = (cq.Workplane("XY", origin=(0, 0, z_bend))
           .polyline(pts).close().extrude(HK_STEP_Z - z_bend))
    # upper section (ball end side)
    arm2 = (cq.Workplane("XY", origin=(0, 0, HK_STEP_Z))
            .polyline(pts_up).close().extrude(HK_SHAFT_TOP - HK_STEP_Z))
    # bend: revolve the hex section about an axis parallel to Y
    bend = (cq.Workplane("XY", origin=(0, 0, z_bend))
            .polyline(pts).close()
            .revolve(90, (HK_BEND_R, 0, 0), (HK_BEND_R, -1, 0)))
    # short leg along +X (profile in YZ plane, corners toward +/-Z)
    leg = (cq.Workplane("YZ", origin=(HK_BEND_R, 0, HK_LEG_Z))
           .polyline([(y, x) for (x, y) in pts]).close()
           .extrude(HK_LEG_END - HK_BEND_R))
    leg = leg.faces(">X").edges().chamfer(HK_TIP_CH)
    # neck + hex ball
    zc = HK_TOP - HK_BALL_R
    z_neck = zc - math.sqrt(HK_BALL_R ** 2 - HK_NECK_R ** 2)
    prof = (cq.Workplane("XZ")
            .moveTo(0, HK_SHAFT_TOP - 0.3)
            .lineTo(HK_AF / 2 * 0.92, HK_SHAFT_TOP - 0.3)
            .lineTo(HK_NECK_R, z_neck - 1.4)
            .lineTo(HK_NECK_R, z_neck)
            .threePointArc((HK_BALL_R, zc), (0, HK_TOP))
            .close())
    ball = prof.revolve(360, (0, 0, 0), (0, 1, 0))
    hexcut = (cq.Workplane("XY", origin=(0, 0, HK_SHAFT_TOP - 1.0))
              .polyline(hexagon_pts(HK_BALL_R * 1.06, HK_ROT)).close().extrude(HK_TOP))
    ball = ball.intersect(hexcut)
    key = arm.union(arm2).union(bend).union(leg).union(ball)
    return key


# ================= 2. rod end =================
def make_rod_end():
    # built along +X from the hex end, eye axis along Y
    r_hex = RE_HEX_AF / math.sqrt(3.0)
    hex_pts = hexagon_pts(r_hex, 90)            # flats at +/-Y
    hx = (cq.Workplane("YZ").polyline(hex_pts).close().extrude(RE_HEX_L))
    # 30 deg nut chamfer on both ends (intersection with a chamfered cylinder)
    r0 = RE_HEX_AF / 2 * 0.96
    c = (r_hex - r0) * math.tan(math.radians(30))
    chamf = (cq.Workplane("XY")
             .polyline([(0, 0), (0, r0), (c, r_hex + 0.01),
                        (RE_HEX_L - c, r_hex + 0.01),
                        (RE_HEX_L, r0), (RE_HEX_L, 0)]).close()
             .revolve(360, (0, 0, 0), (1, 0, 0)))
    hx = hx.intersect(chamf)
    shank = (cq.Workplane("YZ", origin=(RE_HEX_L - 0.1, 0, 0))
             .circle(RE_SHANK_D / 2).extrude(RE_EYE_X - RE_HEX_L))
    eye = (cq.Workplane("XZ", origin=(RE_EYE_X, RE_EYE_T / 2, 0))
           .circle(RE_EYE_R).extrude(RE_EYE_T))
    eye = eye.edges().fillet(RE_EYE_FILLET)
    body = hx.union(shank)
    # flats on the shank where it runs into the eye
    for sy in (1, -1):
        body = body.cut(cq.Workplane("XY")
                        .box(RE_EYE_X, 10, 30, centered=(False, True, True))
                        .translate((RE_FLAT_X, sy * (RE_EYE_T / 2 + 5), 0)))
    body = body.union(eye)
    # housing bore
    body = body.cut(cq.Workplane("XZ", origin=(RE_EYE_X, 20, 0))
                    .circle(RE_HOUSING_R).extrude(40))
    # spherical ball, truncated, with bore
    ball = cq.Workplane("XY").sphere(RE_BALL_SR).translate((RE_EYE_X, 0, 0))
    slab = cq.Workplane("XY").box(2 * RE_BALL_SR + 2, RE_BALL_W, 2 * RE_BALL_SR + 2)\
        .translate((RE_EYE_X, 0, 0))
    ball = ball.intersect(slab)
    ball = ball.cut(cq.Workplane("XZ", origin=(RE_EYE_X, 20, 0))
                    .circle(RE_BORE_R).extrude(40))
    body = body.union(ball)
    # female thread bore in hex end
    body = body.cut(cq.Workplane("YZ", origin=(-1, 0, 0)).circle(4.5).extrude(14))
    body = body.rotate((0, 0, 0), (0, 1, 0), RE_ANGLE)
    return body.translate((RE_START[0], RE_Y, RE_START[1]))


# ================= 3. bushing =================
def make_bushing():
    L = BU_X1 - BU_X0
    b = cq.Workplane("YZ").circle(BU_R).extrude(L)
    b = b.edges().chamfer(0.6)
    b = b.cut(cq.Workplane("YZ", origin=(-1, 0, 0)).circle(BU_BORE_R).extrude(L + 2))
    for x0 in (-1.0, L - 1.2):          # both end faces
        ring = (cq.Workplane("YZ", origin=(x0, 0, 0))
                .circle(BU_SEAL_RO).circle(BU_SEAL_RI).extrude(2.2))
        b = b.cut(ring)
        inner = (cq.Workplane("YZ", origin=(x0, 0, 0))
                 .circle(BU_SEAL_RI - 0.6).circle(BU_BORE_R).extrude(1.6))
        b = b.cut(inner)
    return b.translate((BU_X0, BU_YC, BU_ZC))


# ================= 4. angle bracket =================
def make_angle_bracket():
    front = cq.Workplane("XY").box(AB_W, AB_T, AB_H, centered=False)
    side = cq.Workplane("XY").box(AB_T, AB_D, AB_H, centered=False)
    br = front.union(side)
    br = br.translate((-AB_W / 2, 0, -AB_H / 2))
    br = br.rotate((0, 0, 0), (0, 1, 0), AB_ANGLE)
    return br.translate((AB_CX, Y_TABLE, AB_CZ))


# ================= 5. flange bearing =================
def flange_outline(wp):
    phi = math.acos((FB_RC - FB_RE) / FB_HOLE_D)
    cp, sp = math.cos(phi), math.sin(phi)
    d, R, r = FB_HOLE_D, FB_RC, FB_RE
    w = (wp.moveTo(d + r * cp, -r * sp)
         .threePointArc((d + r, 0), (d + r * cp, r * sp))
         .lineTo(R * cp, R * sp)
         .threePointArc((0, R), (-R * cp, R * sp))
         .lineTo(-d - r * cp, r * sp)
         .threePointArc((-d - r, 0), (-d - r * cp, -r * sp))
         .lineTo(-R * cp, -R * sp)
         .threePointArc((0, -R), (R * cp, -R * sp))
         .close())
    return w


def make_flange_bearing():
    # XZ workplane normal is -Y; extrude toward +Y by using negative offset
    y_front = FB_Y_FRONT + FB_BOSS_H
    body = flange_outline(cq.Workplane("XZ", origin=(0, y_front, 0))).extrude(-FB_T)
    body = body.faces("<Y").edges().chamfer(0.6)
    # front ring boss
    ring = (cq.Workplane("XZ", origin=(0, y_front + 0.01, 0))
            .circle(FB_RING_RO).extrude(FB_BOSS_H))
    body = body.union(ring)
    # back bearing seat: annular recess around the bearing inner ring
    body = body.cut(cq.Workplane("XZ", origin=(0, y_front + FB_T + 1.0, 0))
                    .circle(FB_SEAT_RO).circle(FB_SEAT_RI).extrude(1.0 + FB_SEAT_D))
    # bearing recess & bore
    body = body.cut(cq.Workplane("XZ", origin=(0, FB_Y_FRONT - 1, 0))
                    .circle(FB_RING_RI).circle(FB_RING_RI - 1.0).extrude(-2.2))
    body = body.cut(cq.Workplane("XZ", origin=(0, 30, 0)).circle(FB_BORE_R).extrude(60))
    # bolt holes
    for sx in (-1, 1):
        body = body.cut(cq.Workplane("XZ", origin=(sx * FB_HOLE_D, 30, 0))
                        .circle(FB_BOLT_D / 2).extrude(60))
    body = body.rotate((0, 0, 0), (0, 1, 0), FB_ANGLE)
    return body.translate((FB_CX, 0, FB_CZ))


# ================= 6. handle =================
def make_handle():
    bar = cq.Workplane("XY").box(HD_L, HD_T, HD_H, centered=False)
    x0, x1 = HD_END_L, HD_L - HD_END_R          # end walls
    # middle top lowered behind a thin front lip
    step = cq.Workplane("XY").box(x1 - x0, HD_T - HD_LIP, HD_STEP, centered=False)\
        .translate((x0, HD_LIP, HD_H - HD_STEP))
    bar = bar.cut(step)
    # back channel under the top rim (front wall HD_WALL thick)
    z_top = HD_H - HD_STEP - HD_RIM
    pocket = cq.Workplane("XY").box(x1 - x0, HD_T - HD_WALL + 1, z_top - HD_BASE_H,
                                    centered=False)\
        .translate((x0, HD_WALL, HD_BASE_H))
    bar = bar.cut(pocket)
    # row of small teeth hanging under the rim
    n_teeth = 14
    pitch = (x1 - x0 - 4) / (n_teeth - 1)
    for i in range(n_teeth):
        t = cq.Workplane("XY").box(0.9, HD_T - HD_WALL - 1.0, 2.5, centered=False)\
            .translate((x0 + 2 + i * pitch - 0.45, HD_WALL - 0.01, z_top - 2.49))
        bar = bar.union(t)
    # base plate, trapezoid in plan with 45 deg end
    base = (cq.Workplane("XY")
            .polyline([(0, HD_BASE_Y0), (HD_L, HD_BASE_Y0),
                       (HD_L - (HD_BASE_Y1 - HD_BASE_Y0), HD_BASE_Y1),
                       (HD_BASE_Y1 - HD_BASE_Y0, HD_BASE_Y1)]).close()
            .extrude(HD_BASE_H))
    h = bar.union(base)
    plan = (cq.Workplane("XY", origin=(0, 0, -10))
            .polyline([(0, HD_BASE_Y0), (HD_L, HD_BASE_Y0),
                       (HD_L - (HD_BASE_Y1 - HD_BASE_Y0), HD_BASE_Y1),
                       (HD_BASE_Y1 - HD_BASE_Y0, HD_BASE_Y1)]).close()
            .extrude(20))
    # rail under the base with chamfered ends
    rail = (cq.Workplane("XZ", origin=(0, HD_BASE_Y1 - 0.01, 0))
            .polyline([(HD_RAIL_X0, 0.01), (HD_RAIL_X1, 0.01),
                       (HD_RAIL_X1 - HD_RAIL_H, -HD_RAIL_H),
                       (HD_RAIL_X0 + HD_RAIL_H, -HD_RAIL_H)]).close()
            .extrude(HD_BASE_Y1 - HD_RAIL_Y0 - 0.02))
    h = h.union(rail.intersect(plan))
    # clevis lugs with cross holes
    for lx in HD_LUGS:
        lug = cq.Workplane("XY").box(HD_LUG_W, HD_LUG_Y1 - HD_RAIL_Y0, HD_LUG_TOP + HD_RAIL_H,
                                     centered=False)\
            .translate((lx, HD_RAIL_Y0, -HD_RAIL_H))
        lug = lug.edges("|X and >Y").fillet(2.0)
        h = h.union(lug)
    h = h.cut(cq.Workplane("YZ", origin=(-5, HD_HOLE_Y, HD_HOLE_Z)).circle(HD_HOLE_D / 2)
              .extrude(HD_L + 10))
    # pin end protruding from the outer lug
    pin = cq.Workplane("YZ", origin=(HD_LUGS[1] + 1.0, HD_HOLE_Y, HD_HOLE_Z))\
        .circle(HD_HOLE_D / 2 - 0.1).extrude(HD_LUG_W + 1.5)
    head = cq.Workplane("YZ", origin=(HD_LUGS[1] + HD_LUG_W - 0.01, HD_HOLE_Y, HD_HOLE_Z))\
        .circle(2.4).extrude(2.2)
    head = head.faces(">X").edges().chamfer(0.5)
    h = h.union(pin).union(head)
    h = h.rotate((0, 0, 0), (0, 1, 0), HD_ANGLE)
    return h.translate(HD_ORIGIN)


parts = [
    make_hex_key(),
    make_rod_end(),
    make_bushing(),
    make_angle_bracket(),
    make_flange_bearing(),
    make_handle(),
]

# all six separate bodies, in their relative positions, as one compound
result = cq.Workplane("XY").newObject(
    [cq.Compound.makeCompound([s for p in parts for s in p.solids().vals()])])

VIEW = {"azimuth": 45, "elevation": 26}
